import cadquery as cq
from cadquery.occ_impl.shapes import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
W, H = 120.0, 84.0          # outer width (X) and height (Z)
# plan-view (XZ) corner radii: top-left, top-right, bottom-left, bottom-right
RC_TL, RC_TR, RC_BL, RC_BR = 13.5, 14.0, 14.0, 12.0
# back profile seen from above (x, y), right end to left end:
#   slightly crowned right end -> flat thick part -> S-shaped step down
#   to the gently sloping thin left part
BACK_RIGHT = [(62.0, 18.2), (47.0, 19.6)]
BACK_RIGHT_TAN = [(-1.0, 0.16), (-1.0, 0.0)]
X_FLAT = 32.0               # end of the flat thick part
BACK_STEP = [(13.6, 18.8), (5.1, 16.9), (-4.0, 15.1), (-30.0, 14.3),
             (-49.0, 13.55), (-62.0, 12.3)]
BACK_STEP_TAN = [(-1.0, 0.0), (-1.0, -0.15)]
T_MAX = 19.6                # max back depth
R_BACK = 9.5                # rounding of the top / bottom back edges
R_LEFT = 4.5                # rounding of the left back edge
R_RIGHT = 8.0               # rounding of the right back edge
WALL = 1.35                 # shell wall thickness

Y_RIB = 6.5                 # front plane of the internal ribs
RIB_T = 1.0                 # rib thickness
Z_HRIB = 9.6                # horizontal rib height
X_VRIB_TOP = 14.2           # vertical rib in upper compartment
X_VRIB_L = -51.3            # lower-left vertical rib
X_VRIB_R = 45.8             # lower-right vertical rib
WEB_T = 0.9                 # thickness of the small support webs

BIG_HOLE = (-3.4, 24.6, 12.3, 1.1)   # x, z, diameter, outer countersink
SMALL_HOLE = (34.7, 23.3, 8.3, 0.9)
GRID_X0, GRID_NX, GRID_PX = -42.3, 12, 2.72
GRID_Z0, GRID_NZ, GRID_PZ = 32.6, 5, 3.85
GRID_D = 1.1
PIN_HOLES = [(-44.8, 5.7), (-44.8, -2.0)]
PIN_HOLE_D = 1.2

# screw bosses: x, z, outer dia, hole dia, front y, web direction
BOSSES = [(-4.8, 36.0, 5.3, 1.7, 0.3, None),
          (53.4, -4.8, 5.0, 1.7, 0.3, "+x"),
          (15.0, -35.3, 5.3, 1.7, 0.3, "-z")]
# locating pins: x, z, dia, hole dia (0 = solid), front y, web direction
PINS = [(20.4, 15.6, 2.4, 1.0, 8.4, "-x"),
        (-45.7, -36.5, 1.9, 0.0, 2.3, "-z"),
        (2.4, -37.1, 1.9, 0.0, 2.8, "-z")]
PIN_CHAMFER = 0.5

# rectangular slot through the bottom wall
SLOT = (-38.9, 5.6, 6.8, 3.0)   # x, y centre, x length, y width

VIEW = {"azimuth": 45, "elevation": 26}


def back_spline():
    return (cq.Workplane("XY").moveTo(*BACK_RIGHT[0])
            .spline(BACK_RIGHT[1:], tangents=BACK_RIGHT_TAN, includeCurrent=True)
            .lineTo(X_FLAT, BACK_RIGHT[-1][1])
            .spline(BACK_STEP, tangents=BACK_STEP_TAN, includeCurrent=True))


def back_y(x):
    """Y of the outer back surface at a given x (mid-height)."""
    for e in back_spline().ctx.pendingEdges:
        xa, xb = e.startPoint().x, e.endPoint().x
        if min(xa, xb) <= x <= max(xa, xb):
            lo, hi = 0.0, 1.0
            for _ in range(40):
                mid = (lo + hi) / 2
                if (e.positionAt(mid).x - x) * (xb - xa) < 0:
                    lo = mid
                else:
                    hi = mid
            return e.positionAt(lo).y
    return T_MAX


def outer():
    """Outer skin: rounded rectangle in XZ, crowned / stepped back profile,
    back edges rounded with a radius that varies around the perimeter."""
    x0 = BACK_RIGHT[0][0]
    x1 = BACK_STEP[-1][0]
    prof = (back_spline()
            .lineTo(x1, 0.0).lineTo(x0, 0.0).close()
            .extrude(H / 2 + 2, both=True))
    rr = cq.Workplane("XZ").rect(W, H).extrude(-(T_MAX + 5))
    for sx, sz, r in ((-1, 1, RC_TL), (1, 1, RC_TR), (-1, -1, RC_BL), (1, -1, RC_BR)):
        rr = (rr.edges("|Y")
              .edges(cq.selectors.NearestToPointSelector((sx * W / 2, 5.0, sz * H / 2)))
              .fillet(r))
    b = prof.intersect(rr).val()

    # variable-radius fillet of the closed back edge loop
    probe = cq.Vertex.makeVertex(0.0, back_y(0.0), H / 2)
    start = min(b.Edges(), key=lambda e: e.distance(probe))
    mk = BRepFilletAPI_MakeFillet(b.wrapped)
    mk.Add(R_BACK, start.wrapped)
    n = mk.NbEdges(1)
    edges = [cq.Edge(mk.Edge(1, j)) for j in range(1, n + 1)]

    def rad(p):
        if p.x < -W / 2 + 1:
            return R_LEFT
        if p.x > W / 2 - 1:
            return R_RIGHT
        return R_BACK

    for j in range(n):
        e, prev = edges[j], edges[j - 1]
        p0, p1 = e.startPoint(), e.endPoint()
        pv = (prev.startPoint(), prev.endPoint())
        # orient the edge along the fillet spine (start = shared with prev)
        if min((p0 - q).Length for q in pv) > min((p1 - q).Length for q in pv):
            p0, p1 = p1, p0
        r0, r1 = rad(p0), rad(p1)
        if abs(r0 - r1) < 1e-9:
            mk.SetRadius(r0, 1, j + 1)
        else:
            mk.SetRadius(r0, r1, 1, j + 1)
    mk.Build()
    return cq.Workplane("XY").add(cq.Shape.cast(mk.Shape()))


def ycyl(x, z, d, y0, y1):
    """Cylinder along +Y from y0 to y1 centred at (x, z)."""
    return (cq.Workplane("XZ").workplane(offset=-y0).center(x, z)
            .circle(d / 2).extrude(-(y1 - y0)))


def ybox(x0, x1, z0, z1, y0, y1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


body = outer()
shell = body.faces("<Y").shell(-WALL)

DEP = T_MAX + 5
ZT, ZB = H / 2, -H / 2
XL, XR = -W / 2, W / 2

# ---------------- internal ribs ----------------
ribs = ybox(XL, XR, Z_HRIB - RIB_T / 2, Z_HRIB + RIB_T / 2, Y_RIB, DEP)
ribs = ribs.union(ybox(X_VRIB_TOP - RIB_T / 2, X_VRIB_TOP + RIB_T / 2,
                       Z_HRIB, ZT, Y_RIB, DEP))
for xr in (X_VRIB_L, X_VRIB_R):
    ribs = ribs.union(ybox(xr - RIB_T / 2, xr + RIB_T / 2, ZB, Z_HRIB, Y_RIB, DEP))


def web(x, z, yf, direction):
    """Thin support web from a boss/pin to the nearest wall or rib."""
    h = WEB_T / 2
    if direction == "-z":
        return ybox(x - h, x + h, ZB, z, yf + 0.3, DEP)
    if direction == "+x":
        return ybox(x, XR, z - h, z + h, yf + 0.3, DEP)
    if direction == "-x":
        return ybox(X_VRIB_TOP, x, z - h, z + h, yf + 0.3, DEP)
    return None


for (x, z, d, dh, yf, wd) in BOSSES:
    ribs = ribs.union(ycyl(x, z, d, yf, DEP))
    if wd:
        ribs = ribs.union(web(x, z, yf, wd))
for (x, z, d, dh, yf, wd) in PINS:
    pin = ycyl(x, z, d, yf, DEP)
    if dh == 0:
        pin = pin.faces("<Y").edges().chamfer(PIN_CHAMFER)
    ribs = ribs.union(pin)
    if wd:
        ribs = ribs.union(web(x, z, yf, wd))

ribs = ribs.intersect(body)
part = shell.union(ribs)

# boss / pin holes (blind)
for (x, z, d, dh, yf, wd) in BOSSES:
    part = part.cut(ycyl(x, z, dh, yf - 1, yf + 9))
for (x, z, d, dh, yf, wd) in PINS:
    if dh > 0:
        part = part.cut(ycyl(x, z, dh, yf - 1, yf + 5))

# ---------------- through holes in the back ----------------
cut = None
for (hx, hz, hd, cs) in (BIG_HOLE, SMALL_HOLE):
    c = ycyl(hx, hz, hd, 0, DEP)
    yb = back_y(hx)
    cone = cq.Solid.makeCone(hd / 2, hd / 2 + cs + 3.0, cs + 3.0,
                             cq.Vector(hx, yb - cs, hz), cq.Vector(0, 1, 0))
    c = c.union(cq.Workplane("XY").add(cone))
    cut = c if cut is None else cut.union(c)
pts = [(GRID_X0 + i * GRID_PX, GRID_Z0 - j * GRID_PZ)
       for i in range(GRID_NX) for j in range(GRID_NZ)]
cut = cut.union(cq.Workplane("XZ").workplane(offset=-5).pushPoints(pts)
                .circle(GRID_D / 2).extrude(-DEP))
cut = cut.union(cq.Workplane("XZ").workplane(offset=-5).pushPoints(PIN_HOLES)
                .circle(PIN_HOLE_D / 2).extrude(-DEP))
# slot through the bottom wall
sx, sy, sl, sw = SLOT
cut = cut.union(ybox(sx - sl / 2, sx + sl / 2, ZB - 1, ZB + 4.0,
                     sy - sw / 2, sy + sw / 2))
part = part.cut(cut)

result = part
